import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_OUT = 50.0          # ring outer radius
WALL = 3.0            # ring wall thickness
R_IN = R_OUT - WALL   # ring inner radius
H = 25.5              # ring height
SEAM_OUT = 225.0      # angle of the outer cylinder seam (cosmetic)
SEAM_IN = 90.0        # angle of the inner cylinder seams (hidden at a latch)
REBATE_R = 48.3       # inner rebate at the bottom of the ring wall
REBATE_H = 2.3

# vent grid (square through holes in the ring wall, centred near +X)
VENT = 1.6            # square hole size
VENT_COLS = 7
VENT_ROWS = 6
VENT_PITCH_Z = 4.05
VENT_PITCH_T = 4.05   # pitch along the circumference
VENT_Z0 = 3.5         # centre height of the lowest row
VENT_ANG0 = 0.85      # small angular offset of the grid centre (deg)

# tray (open box attached to the +X side of the ring)
TRAY_X0 = -17.0       # outer face of the -X end wall
TRAY_HALF_W = 17.2    # half width (Y)
TRAY_T = 2.5          # wall thickness
TRAY_TOP = 24.0       # top of tray walls
TRAY_BOT = 0.0        # underside of tray floor
TRAY_FLOOR = 2.0      # floor thickness
TRAY_FLOOR_R = 45.0   # floor ends on this radius (gap to the ring)
HOLE_D = 12.4         # round hole in the -X end wall
HOLE_Y = -0.2
HOLE_Z = 13.5

# snap latches (two, 180 deg apart on the Y axis); profiles are in (r, z)
LATCH_W = 11.3        # width along X of the hook body
LATCH_R_IN = 34.7     # inner radius of hook body
LATCH_TOP = H + 11.6  # top of hook above the rim
LATCH_ZB_IN = 24.5    # underside height at the inner face
LATCH_R_KNEE = 44.0   # radius where the sloped underside becomes flat
LATCH_ZB_OUT = 16.4   # flat underside height next to the ring wall
LATCH_FILLET = 1.2    # round on the outer top edge of the hook
WIN_R0 = 37.2         # window inner radius
WIN_R1 = 44.45       # window outer radius
WIN_TOP = LATCH_TOP - 1.7
WIN_BOT = H
WIN_CH_R = 4.1        # chamfer of the window's top outer corner
WIN_CH_Z = 3.7

GUIDE_W = 10.5        # guide block beside the hook (on the other side of the axis)
GUIDE_R0 = 37.5
GUIDE_R1 = 45.6
GUIDE_TOP = 14.7
GUIDE_SLOPE_Z = 10.0  # sloped outer face meets the ring wall at this height
GUIDE_BOT = 0.0       # guide runs down to the bottom of the ring

FOOT_W = 12.9         # foot block under the hook (same side as the hook)
FOOT_R0 = 38.5        # inner radius of the foot
FOOT_R1 = 44.8        # outer radius of the foot (gap to the ring wall)
FOOT_TOP = 9.0
FOOT_FLAT = 2.0       # flat part of the foot top before it slopes down
FOOT_Z_OUT = 5.2      # top height at the outer face


def annulus(r0, r1, z0, z1):
    return (cq.Workplane("XY").workplane(offset=z0)
            .circle(r1).circle(r0).extrude(z1 - z0))


def revolved(pts):
    """solid of revolution about Z from a closed (r, z) polyline"""
    return (cq.Workplane("XZ").polyline(pts).close()
            .revolve(360, (0, 0, 0), (0, 1, 0)))


def slab_x(x0, x1, z0=-5.0, z1=60.0):
    return (cq.Workplane("XY").workplane(offset=z0)
            .center((x0 + x1) / 2, R_OUT / 2)
            .rect(x1 - x0, R_OUT + 4).extrude(z1 - z0))


# ---------------- ring ----------------
def cyl(r, z0, z1, seam):
    return (cq.Workplane("XY").workplane(offset=z0).circle(r).extrude(z1 - z0)
            .rotate((0, 0, 0), (0, 0, 1), seam))


ring = (cyl(R_OUT, 0, H, SEAM_OUT)
        .cut(cyl(R_IN, -1, H + 1, SEAM_IN))
        .cut(cyl(REBATE_R, -1, REBATE_H, SEAM_IN)))

# ---------------- tray ----------------
tray_len = R_OUT - 1.0 - TRAY_X0
tray_outer = (cq.Workplane("XY").workplane(offset=TRAY_BOT)
              .center(TRAY_X0 + tray_len / 2, 0)
              .rect(tray_len, 2 * TRAY_HALF_W).extrude(TRAY_TOP - TRAY_BOT))
tray_inner = (cq.Workplane("XY").workplane(offset=TRAY_BOT + TRAY_FLOOR)
              .center(TRAY_X0 + TRAY_T + tray_len / 2, 0)
              .rect(tray_len, 2 * (TRAY_HALF_W - TRAY_T)).extrude(TRAY_TOP))
tray = tray_outer.cut(tray_inner)
# floor stops short of the ring wall: annular gap through the floor
gap = annulus(TRAY_FLOOR_R, REBATE_R + 1.0, TRAY_BOT - 1, TRAY_BOT + TRAY_FLOOR + 0.01)
gap = gap.intersect(cq.Workplane("XY").workplane(offset=TRAY_BOT - 1)
                    .center(30, 0).rect(40, 2 * (TRAY_HALF_W - TRAY_T))
                    .extrude(TRAY_FLOOR + 2))
tray = tray.cut(gap)
tray = tray.intersect(cq.Workplane("XY").circle(R_IN + 0.5).extrude(H))
hole = (cq.Workplane("YZ").workplane(offset=TRAY_X0 - 1)
        .center(HOLE_Y, HOLE_Z).circle(HOLE_D / 2).extrude(TRAY_T + 2))
tray = tray.cut(hole)


# ---------------- latch (built at +Y, copied at 180 deg) ----------------
def make_latch():
    hook = revolved([(LATCH_R_IN, LATCH_ZB_IN), (LATCH_R_KNEE, LATCH_ZB_OUT),
                     (R_IN, LATCH_ZB_OUT), (R_IN, LATCH_TOP),
                     (LATCH_R_IN, LATCH_TOP)])
    hook = hook.intersect(slab_x(0.0, LATCH_W))
    if LATCH_FILLET > 0:
        hook = (hook.faces(">Z").edges("%CIRCLE")
                .edges(cq.selectors.RadiusNthSelector(1)).fillet(LATCH_FILLET))
    win = revolved([(WIN_R0, WIN_BOT), (WIN_R1, WIN_BOT),
                    (WIN_R1, WIN_TOP - WIN_CH_Z), (WIN_R1 - WIN_CH_R, WIN_TOP),
                    (WIN_R0, WIN_TOP)])
    win = win.intersect(slab_x(-1.0, LATCH_W + 1.0))
    hook = hook.cut(win)
    k = (GUIDE_TOP - GUIDE_SLOPE_Z) / (R_IN - GUIDE_R1)
    guide = revolved([(GUIDE_R0, GUIDE_BOT), (GUIDE_R0, GUIDE_TOP),
                      (GUIDE_R1, GUIDE_TOP), (R_IN + 0.5, GUIDE_SLOPE_Z - 0.5 * k),
                      (R_IN + 0.5, GUIDE_BOT)])
    guide = guide.intersect(slab_x(-GUIDE_W, 0.0))
    foot = revolved([(FOOT_R0, 0.0), (FOOT_R0, FOOT_TOP),
                     (FOOT_R0 + FOOT_FLAT, FOOT_TOP),
                     (FOOT_R1, FOOT_Z_OUT), (FOOT_R1, 0.0)])
    foot = foot.intersect(slab_x(-0.5, FOOT_W))
    return [hook, guide, foot]


part = ring.union(tray)
for piece in make_latch():
    part = part.union(piece)
    part = part.union(piece.rotate((0, 0, 0), (0, 0, 1), 180))

# ---------------- vents ----------------
dth = math.degrees(VENT_PITCH_T / R_OUT)
cutters = []
for i in range(VENT_COLS):
    ang = VENT_ANG0 + (i - (VENT_COLS - 1) / 2) * dth
    for j in range(VENT_ROWS):
        z = VENT_Z0 + j * VENT_PITCH_Z
        cutters.append(cq.Solid.makeBox(WALL + 4, VENT, VENT,
                                        cq.Vector(R_OUT - WALL - 2, -VENT / 2, z - VENT / 2))
                       .rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), ang))
part = part.cut(cq.Workplane("XY").add(cq.Compound.makeCompound(cutters)))

result = part
